import math
import cadquery as cq
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet

# =====================================================================
#  Curved handle / lever with a clevis hinge at its rear end
#  Body: rounded box swept on a plan arc (convex towards +X),
#  rear: flat tongue plate + two pierced lugs, slots in both ends.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
H = 26.5            # body height
W = 17.3            # body width
RC = 116.0          # centre-line radius of the curved part of the body (plan view)
ANG_FRONT = 23.0    # arc sweep in front of the apex (deg)
ANG_REAR = 15.5     # arc sweep behind the apex (deg) = plan angle of the straight rear part
L_STRAIGHT = 13.8   # straight rear part of the body (tangent to the arc)
EDGE_R = 3.2        # rounding of the long edges of the body
END_R = 3.5         # rounding of the end edges of the body

SLOT_T = 2.6        # thickness of the end slots
SLOT_Z = H / 2.0    # height of the end slots
SLOT_D_IN = 7.5     # front slot depth at the inner (-X) side
SLOT_D_OUT = 4.5    # front slot depth at the outer (+X) side
SLOT_D_REAR = 4.0   # depth of the rear end slot

PLATE_L = 26.8      # plate length beyond the rear end of the body
PLATE_W = W         # plate width (flush with the body)
PLATE_T = 6.0       # plate thickness
PLATE_R = 5.0       # plan corner radius of the plate end
PLATE_OVL = 0.5     # plate overlap into the body (= lug root position)
PLATE_BOT_R = 2.5   # rounding of the plate underside edges
PLATE_TOP_R = 0.6   # rounding of the plate top edges
NECK_R = 5.0        # concave blend under the plate (body end frame)

LUG_GAP = 7.2       # gap between the lugs
PIN_Y = 5.1         # pin axis position beyond the rear end
PIN_Z = H + 8.9     # pin axis height
LUG_RTOP = 2.9      # radius of the lug top
LUG_A0 = 215.0      # angle where the round top meets the S shaped front edge
PIN_D = 2.9         # pin hole diameter
LUG_FRONT = 7.0     # lug root reaches this far in front of the pin
LUG_BACK_R = 3.4    # concave root blend at the back of the lug
U_R = 5.4           # root radius of the lug inner faces (they meet in a V)

HOLE_D = 2.3        # small holes
HOLE_DEPTH = 5.0
HOLE_FRONT = 4.0    # top hole position from the front end
HOLE_REAR = 3.4     # top hole position before the rear end
HOLE_PLATE = 18.5   # hole under the plate, beyond the rear end

GROOVE_W = 3.5      # stepped groove across the plate top: wide shallow part ...
GROOVE_D = 1.5
GROOVE_W2 = 1.2     # ... plus a narrow deeper slot along its +x edge
GROOVE_D2 = 3.0
GROOVE_ANG = 32.0   # groove angle to the plate axis
GROOVE_X0 = 0.3     # groove centre where it leaves the far plate end

c45 = math.cos(math.radians(45))


def place(shape, pt, rot_deg):
    """place a shape built in a local frame (x across, y along the body, z up)"""
    return shape.rotate((0, 0, 0), (0, 0, 1), rot_deg).translate((pt[0], pt[1], 0))


thf = math.radians(ANG_FRONT)
thr = math.radians(ANG_REAR)
FRONT_PT = (-RC + RC * math.cos(thf), -RC * math.sin(thf))          # front end, centre line
REAR_PT = (-RC + RC * math.cos(thr) - L_STRAIGHT * math.sin(thr),  # rear end, centre line
           RC * math.sin(thr) + L_STRAIGHT * math.cos(thr))


def front(shape):
    return place(shape, FRONT_PT, -ANG_FRONT)


def rear_frame(shape):
    return place(shape, REAR_PT, ANG_REAR)


# ---------------- curved body ----------------
SWEEP = ANG_FRONT + ANG_REAR
arc_part = (
    cq.Workplane("XZ")
    .pushPoints([(RC, H / 2.0)])
    .rect(W, H)
    .revolve(SWEEP, (0, 0, 0), (0, 1, 0))
)
# raw body: arc spans angle 0 (front end, in the XZ plane) .. SWEEP, then a straight part
ra = math.radians(SWEEP)
arc_end = (RC * math.cos(ra), RC * math.sin(ra))
straight = (
    cq.Workplane("XY")
    .box(W, L_STRAIGHT, H, centered=(True, False, False))
    .rotate((0, 0, 0), (0, 0, 1), SWEEP)
    .translate((arc_end[0], arc_end[1], 0))
)
raw = arc_part.union(straight)
raw_rear = (arc_end[0] - L_STRAIGHT * math.sin(ra), arc_end[1] + L_STRAIGHT * math.cos(ra))

# rear end slot (cut before rounding so the lower rear corners can be rounded)
slot_r = (
    cq.Workplane("XY")
    .box(W + 10, SLOT_D_REAR + 5, SLOT_T, centered=(True, False, True))
    .translate((0, -SLOT_D_REAR, SLOT_Z))
    .rotate((0, 0, 0), (0, 0, 1), SWEEP)
    .translate((raw_rear[0], raw_rear[1], 0))
)
raw = raw.cut(slot_r).val()


def rear_dist(p):
    # signed distance of a point from the rear end plane
    return -(p.x - raw_rear[0]) * math.sin(ra) + (p.y - raw_rear[1]) * math.cos(ra)


def edge_radius(e):
    """rounding radius for an edge of the raw body, None = keep sharp"""
    if e.geomType() not in ("CIRCLE", "LINE"):
        return None
    c = e.Center()
    bb = e.BoundingBox()
    on_front = bb.ylen < 1e-6 and abs(c.y) < 1e-6
    on_rear = (e.geomType() == "LINE" and abs(rear_dist(c)) < 1e-6
               and abs(rear_dist(e.startPoint())) < 1e-6)
    if on_front:
        # front end: all edges except the inner vertical one, which stays sharp
        if abs(c.x - (RC - W / 2)) < 1e-6 and bb.zlen > H - 1e-6:
            return None
        return END_R
    if on_rear:
        # rear end: bottom edge and the vertical edges below the slot
        # (the top one is covered by the plate, the upper ones by the neck)
        if abs(c.z) < 1e-6:
            return END_R
        if bb.zlen > 1.0 and bb.zmax < SLOT_Z:
            return EDGE_R
        return None
    if bb.zlen < 1e-6 and (c.z < 1e-6 or c.z > H - 1e-6):
        return EDGE_R                         # the four long edges (arc + straight part)
    return None


rounded = [(e, edge_radius(e)) for e in raw.Edges()]
rounded = [(e, r) for e, r in rounded if r is not None]
mk = BRepFilletAPI_MakeFillet(raw.wrapped)
for e, r in rounded:
    mk.Add(r, e.wrapped)
mk.Build()
if mk.IsDone():
    body_s = cq.Solid(mk.Shape())
else:                                         # fallback: one common radius
    body_s = raw.fillet(EDGE_R, [e for e, r in rounded])
body = (
    cq.Workplane("XY")
    .add(body_s)
    .rotate((0, 0, 0), (0, 0, 1), -ANG_FRONT)
    .translate((-RC, 0, 0))
)


# ---------------- rear tongue plate (hinge frame) ----------------
plate = (
    cq.Workplane("XY")
    .box(PLATE_W, PLATE_L + PLATE_OVL, PLATE_T, centered=(True, False, False))
    .translate((0, -PLATE_OVL, H - PLATE_T))
)
plate = plate.edges("|Z and >Y").fillet(PLATE_R)
plate = plate.faces("<Z").edges().filter(lambda e: e.Center().y > 1.0).fillet(PLATE_BOT_R)
plate = plate.faces(">Z").edges().filter(lambda e: e.Center().y > 1.0).fillet(PLATE_TOP_R)

# shallow groove across the plate top, from the far end to the -x side
g_len = 40.0
groove = (
    cq.Workplane("XY")
    .box(GROOVE_W, g_len, GROOVE_D * 2, centered=(True, False, True))
    .union(
        cq.Workplane("XY")
        .box(GROOVE_W2, g_len, GROOVE_D2 * 2, centered=(True, False, True))
        .translate(((GROOVE_W - GROOVE_W2) / 2.0, 0, 0))
    )
    .translate((0, -g_len, 0))
    .rotate((0, 0, 0), (0, 0, 1), -GROOVE_ANG)
    .translate((GROOVE_X0 + 2.0 * math.tan(math.radians(GROOVE_ANG)), PLATE_L + 2.0, H))
)
plate = plate.cut(groove)

# blind hole under the plate
plate_hole = (
    cq.Workplane("XY")
    .center(0, HOLE_PLATE)
    .circle(HOLE_D / 2.0)
    .extrude(3.0)
    .translate((0, 0, H - PLATE_T - 0.01))
)
plate = plate.cut(plate_hole)

# ---------------- clevis lugs (hinge frame) ----------------
half = W / 2.0                       # lug outer faces flush with the body sides
a0 = math.radians(LUG_A0)
p_w = (PIN_Y + LUG_RTOP * math.cos(a0), PIN_Z + LUG_RTOP * math.sin(a0))  # waist/top joint
t_w = (math.sin(a0), -math.cos(a0))                                          # clockwise tangent there (up, -y)
z_low = min(H - EDGE_R - 0.3, H - PLATE_T + PLATE_BOT_R)   # lug block covers the rounded body edges
y_back = PIN_Y + LUG_RTOP + 0.2 + LUG_BACK_R
lug_prof = (
    cq.Workplane("YZ")
    .moveTo(PIN_Y - LUG_FRONT, z_low)
    .lineTo(PIN_Y - LUG_FRONT, H)
    # S shaped front edge: flared root, slim waist under the round top
    .spline(
        [(PIN_Y - 4.1, PIN_Z - 7.2), (PIN_Y - 2.8, PIN_Z - 4.7), p_w],
        tangents=[(1.0, 0.3), (t_w[0], t_w[1])],
        includeCurrent=True,
    )
    .threePointArc((PIN_Y, PIN_Z + LUG_RTOP), (PIN_Y + LUG_RTOP, PIN_Z))
    .lineTo(PIN_Y + LUG_RTOP + 0.2, H + LUG_BACK_R)
    .threePointArc(
        (y_back - LUG_BACK_R * c45, H + LUG_BACK_R - LUG_BACK_R * c45),
        (y_back, H),
    )
    .lineTo(y_back, z_low)
    .close()
    .extrude(half, both=True)
)
# gap between the lugs: straight inner faces with large root blends meeting in a V
u_box = (
    cq.Workplane("XY")
    .box(LUG_GAP, 40, 30, centered=(True, True, False))
    .translate((0, 5, H + U_R))
)
cx = LUG_GAP / 2.0 - U_R
u_cyl_a = cq.Workplane("XZ").center(cx, H + U_R).circle(U_R).extrude(-40).translate((0, -15, 0))
u_cyl_b = cq.Workplane("XZ").center(-cx, H + U_R).circle(U_R).extrude(-40).translate((0, -15, 0))
u_lens = u_cyl_a.intersect(u_cyl_b)
lugs = lug_prof.cut(u_box).cut(u_lens)
pin = (
    cq.Workplane("YZ")
    .center(PIN_Y, PIN_Z)
    .circle(PIN_D / 2.0)
    .extrude(half + 2, both=True)
)
lugs = lugs.cut(pin)

rear = plate.union(lugs)

# ---------------- concave blend under the plate ----------------
zb = H - PLATE_T
neck = (
    cq.Workplane("YZ")
    .moveTo(-1.0, zb - NECK_R)
    .lineTo(0.0, zb - NECK_R)
    .threePointArc((NECK_R - NECK_R * c45, zb - NECK_R + NECK_R * c45), (NECK_R, zb))
    .lineTo(NECK_R, zb + 0.5)
    .lineTo(-1.0, zb + 0.5)
    .close()
    .extrude(PLATE_W / 2.0, both=True)
)
rear = rear.union(neck)

part = body.union(rear_frame(rear))

# ---------------- front end slot (back wall slanted: deeper on the inner side) ----------------
d_mid = (SLOT_D_IN + SLOT_D_OUT) / 2.0
k = (SLOT_D_IN - SLOT_D_OUT) / W
xs = W / 2.0 + 6.0
slot_f = (
    cq.Workplane("XY")
    .polyline([(-xs, -6.0), (xs, -6.0), (xs, d_mid - k * xs), (-xs, d_mid + k * xs)])
    .close()
    .extrude(SLOT_T)
    .translate((0, 0, SLOT_Z - SLOT_T / 2.0))
)
# front frame: y points from the front end face into the body
part = part.cut(front(slot_f))

# ---------------- small holes in the top face ----------------
hf = (
    cq.Workplane("XY")
    .center(0, HOLE_FRONT)
    .circle(HOLE_D / 2.0)
    .extrude(HOLE_DEPTH)
    .translate((0, 0, H - HOLE_DEPTH + 0.01))
)
part = part.cut(front(hf))
hr = (
    cq.Workplane("XY")
    .center(0, -HOLE_REAR)
    .circle(HOLE_D / 2.0)
    .extrude(HOLE_DEPTH)
    .translate((0, 0, H - HOLE_DEPTH + 0.01))
)
part = part.cut(rear_frame(hr))

result = part

VIEW = {"azimuth": 45, "elevation": 26}
